import cadquery as cq
import math

# =====================================================================
#  Pill-shaped speaker housing
#  front face (-Y) is a flat stadium; the body tapers slightly towards
#  the back along a large arc; vent slots on top, a button pad on the
#  top-front edge, a foot plate with vents and a round button underneath,
#  and an end cap at +X with a deeper (elliptical) front rounding.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 180.0          # length along X at the front face
H = 50.0           # height along Z at the front face (= end diameter)
D = 50.0           # depth along Y (front face at -Y)
TAPER_BACK = 5.0   # how much every side has moved in at the back face
R_FRONT_U = 9.0    # front rounding: extent across the front face
R_FRONT_V = 7.9    # front rounding: extent along the sides (depth)
R_BACK = 1.5       # rounding of the back face edge

# +X end cap with a deeper elliptical front rounding
XC = 70.0          # x position of the end-cap step
R_CAP_U = 9.0      # cap rounding extent across the front face
R_CAP_Y = 15.8     # cap rounding extent along Y (seam position)
SEAM_W = 0.3       # parting groove at the seam
SEAM_DEPTH = 0.2

# top vent slots
N_SLOTS = 21
SLOT_PITCH = 6.05
SLOT_W = 2.8
SLOT_L = 14.8
SLOT_Y0 = 12.9     # distance of slot front end from the front face
SLOT_DEPTH = 1.0   # floor depth of the front part of each slot
SLOT_L2 = 8.6      # length of that shallow front part
SLOT_DEPTH2 = 3.5  # depth of the back part of each slot

# button pad on the top-front edge
PAD_L = 35.5
PAD_Y0 = 3.6       # from the front face
PAD_Y1 = 12.5
PAD_DROP_F = 1.5   # facet depth below the top line (zT) at its front edge
PAD_DROP_B = 0.1   # facet depth below the local top surface at its back edge
PAD_DOT_X = -8.0
PAD_DOT_D = 1.2

# front face domes
DOME_X = 45.3
DOME_D = 5.5
DOME_H = 0.5

# bottom foot plate
PLATE_L = 119.0
PLATE_Y0 = None    # from the front face; None = where the front rounding ends
PLATE_Y1 = 32.3
PLATE_T = 6.0      # plate thickness (reaching up into the body)
PLATE_R = 7.5      # corner radius of the plate
N_BSLOTS = 8       # slots per side on the plate
BSLOT_X0 = 13.0    # first slot centre from the middle
BSLOT_PITCH = 5.75
BSLOT_W = 1.8
BSLOT_L = 14.0
BSLOT_DEPTH = 1.2
BTN_D = 10.0       # round button in the plate centre
BTN_RING_D = 13.4
BTN_RING_DEPTH = 0.8
BTN_DOME_R = 0.7   # rounding of the button rim
MID_W = 15.0       # width of the middle button section
GROOVE_W = 0.5     # split lines around the middle section
GROOVE_DEPTH = 0.4

# ---------------- derived values ----------------
yF = -D / 2.0                    # front face plane
yB = D / 2.0                     # back face plane
RH = H / 2.0                     # half height = end radius at the front
zT = RH                          # top of the body (front section)
zB = -RH                         # bottom of the body (front section)
XE = W / 2.0 - RH                # x of the end-arc centres
R_SIDE = (D ** 2 + TAPER_BACK ** 2) / (2 * TAPER_BACK)   # side taper arc radius
CU = RH - R_SIDE                 # centre (u) of that arc, at the front plane


def side_u(v):
    """distance of the side surface from the centre line, v behind the front"""
    return CU + math.sqrt(R_SIDE ** 2 - v ** 2)


def top_drop(v):
    """how far the side surface has fallen away at depth v"""
    return RH - side_u(v)


def top_slope_deg(v):
    return math.degrees(math.atan(v / math.sqrt(R_SIDE ** 2 - v ** 2)))


def arc_mid(c, p0, p1):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    r = math.hypot(p0[0] - c[0], p0[1] - c[1])
    am = (a0 + a1) / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def half_profile(plane, cap=False):
    """Half section of the housing: u = distance from the centre line,
    v = depth behind the front face.  Front rounding, side taper arc,
    back rounding; closed along the centre line."""
    # back rounding: circle tangent to the back line and inside the side arc
    cb = (CU + math.sqrt((R_SIDE - R_BACK) ** 2 - (D - R_BACK) ** 2), D - R_BACK)
    s = R_SIDE / (R_SIDE - R_BACK)
    t2 = (CU + (cb[0] - CU) * s, cb[1] * s)
    pb = (cb[0], D)
    wp = cq.Workplane(plane).moveTo(0, 0)
    # soft rounding tangent to the front face and to the side arc
    ru, rv = (R_CAP_U, R_CAP_Y) if cap else (R_FRONT_U, R_FRONT_V)
    p0 = (RH - ru, 0.0)
    t1 = (side_u(rv), rv)
    sphi = rv / R_SIDE
    tang = (-sphi, math.sqrt(1 - sphi ** 2))
    wp = wp.lineTo(*p0).spline([t1], tangents=[(1, 0), tang], includeCurrent=True)
    wp = wp.threePointArc(arc_mid((CU, 0.0), t1, t2), t2)
    wp = wp.threePointArc(arc_mid(cb, t2, pb), pb)
    return wp.lineTo(0, D).close()


def end_piece(cap=False):
    """rounded end: the half section revolved about the end-arc axis"""
    pl = cq.Plane(origin=(XE, yF, 0), xDir=(1, 0, 0), normal=(0, 0, 1))
    rev = half_profile(pl, cap).revolve(360, (0, 0, 0), (0, 1, 0))
    keep = cq.Workplane("XY").box(RH * 2, D * 2, H * 2).translate((XE + RH, 0, 0))
    return rev.intersect(keep)


# ---------------- main body ----------------
pl_mid = cq.Plane(origin=(XE, yF, 0), xDir=(0, 0, 1), normal=(-1, 0, 0))
mid_half = half_profile(pl_mid).extrude(2 * XE)
mid = mid_half.union(mid_half.mirror("XY"))

end_r = end_piece(False)
end_l = end_r.mirror("YZ")
# +X end cap: its front part (up to the seam) gets the deeper rounding
cap_r = end_piece(True)
cap_zone = (cq.Workplane("XY").box(W, R_CAP_Y + 5, H * 2)
            .translate((XC + W / 2, yF + R_CAP_Y - (R_CAP_Y + 5) / 2, 0)))
end_r = end_r.cut(cap_zone).union(cap_r.intersect(cap_zone))

body = mid.union(end_r).union(end_l)

# fine parting groove where the end-cap rounding runs out
groove_r = side_u(R_CAP_Y)
seam = (cq.Workplane("XZ", origin=(XE, yF + R_CAP_Y + SEAM_W / 2, 0))
        .circle(groove_r + 5).circle(groove_r - SEAM_DEPTH)
        .extrude(SEAM_W)
        .intersect(cq.Workplane("XY").box(W, D * 2, H * 2)
                   .translate((XC + W / 2, 0, 0))))
body = body.cut(seam)

# ---------------- top vent slots ----------------
slot_xs = [(i - (N_SLOTS - 1) / 2) * SLOT_PITCH for i in range(N_SLOTS)]


def slot_tool(y0, length, depth):
    """row of slots whose floor lies 'depth' below the (sloping) top surface"""
    v_c = y0 + length / 2
    zc = zT - top_drop(v_c)
    tool = (cq.Workplane("XY", origin=(0, yF + v_c, zc - depth))
            .pushPoints([(x, 0) for x in slot_xs])
            .slot2D(length, SLOT_W, 90)
            .extrude(depth + 4))
    return tool.rotate((0, yF + v_c, zc), (1, yF + v_c, zc), -top_slope_deg(v_c))


# whole slot to the shallow floor, then the part behind the shallow front
# floor (bounded by its round back end) down to the deep floor
body = body.cut(slot_tool(SLOT_Y0, SLOT_L, SLOT_DEPTH))
deep = (slot_tool(SLOT_Y0, SLOT_L, SLOT_DEPTH2)
        .cut(slot_tool(SLOT_Y0 - 0.01, SLOT_L2, SLOT_DEPTH2 + 1)))
body = body.cut(deep)

# ---------------- button pad over the top-front edge ----------------
# a flat, slightly tilted stadium-shaped facet sunk into the top-front rounding
pad_cy = yF + (PAD_Y0 + PAD_Y1) / 2
pad_w = PAD_Y1 - PAD_Y0
pad_prism = (cq.Workplane("XY", origin=(0, pad_cy, zT - 10))
             .slot2D(PAD_L, pad_w, 0)
             .extrude(14))
z_front = zT - PAD_DROP_F
z_back = side_u(PAD_Y1) - PAD_DROP_B
ang = math.degrees(math.atan2(z_back - z_front, PAD_Y1 - PAD_Y0))
big = 400.0
above = (cq.Workplane("XY").box(big, big, big)
         .translate((0, 0, big / 2))
         .rotate((0, 0, 0), (1, 0, 0), ang)
         .translate((0, yF + PAD_Y0, z_front)))
body = body.cut(pad_prism.intersect(above))
# small indicator hole on the pad
dot = (cq.Workplane("XY", origin=(PAD_DOT_X, pad_cy - 0.5, zT - 3))
       .circle(PAD_DOT_D / 2).extrude(5))
body = body.cut(dot)

# ---------------- front face domes ----------------
for sx in (-1, 1):
    dome = (cq.Workplane("XZ", origin=(sx * DOME_X, yF + 0.5, 0))
            .circle(DOME_D / 2).extrude(DOME_H + 0.5))
    dome = dome.faces("<Y").edges().fillet(DOME_H * 0.8)
    body = body.union(dome)

# ---------------- bottom foot plate ----------------
# flat foot, flush with the lowest line of the body at its front edge and
# standing proud of the tapering underside further back
if PLATE_Y0 is None:
    PLATE_Y0 = R_FRONT_V
zP = -side_u(PLATE_Y0)            # plane of the foot
plate_cy = yF + (PLATE_Y0 + PLATE_Y1) / 2
plate_d = PLATE_Y1 - PLATE_Y0
plate = (cq.Workplane("XY", origin=(0, plate_cy, zP))
         .rect(PLATE_L, plate_d).extrude(PLATE_T)
         .edges("|Z").fillet(PLATE_R))
body = body.union(plate)

# slots in the plate, two groups either side of the button
bpts = []
for sx in (-1, 1):
    for i in range(N_BSLOTS):
        bpts.append((sx * (BSLOT_X0 + i * BSLOT_PITCH), plate_cy))
bslots = (cq.Workplane("XY", origin=(0, 0, zP - 1))
          .pushPoints(bpts)
          .slot2D(BSLOT_L, BSLOT_W, 90)
          .extrude(BSLOT_DEPTH + 1))
body = body.cut(bslots)

# round button sitting in a recessed ring, with a rounded rim
well = (cq.Workplane("XY", origin=(0, plate_cy, zP - 1))
        .circle(BTN_RING_D / 2).extrude(BTN_RING_DEPTH + 1))
body = body.cut(well)
button = (cq.Workplane("XY", origin=(0, plate_cy, zP))
          .circle(BTN_D / 2).extrude(BTN_RING_DEPTH + 0.5)
          .faces("<Z").edges().fillet(BTN_DOME_R))
body = body.union(button)

# split lines bounding the middle button section
grooves = (cq.Workplane("XY", origin=(0, plate_cy, zP - 1))
           .pushPoints([(-MID_W / 2, 0), (MID_W / 2, 0)])
           .rect(GROOVE_W, plate_d + 2)
           .extrude(GROOVE_DEPTH + 1)
           .intersect(plate))          # keep them within the foot plate
body = body.cut(grooves)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
